import math
import cadquery as cq

VIEW = {"azimuth": 45, "elevation": 26}

# ---- driving dimensions (mm) ----
D = 70.0            # overall base diameter
H = 15.0            # overall height (flat crown)
R_SHOULDER = 15.0   # radius of the rounded shoulder (quarter round from rim to crown)
HOLE_D = 8.1        # through hole diameter
CSK_D = 16.4        # countersink diameter on the underside
CSK_ANGLE = 82.0    # countersink included angle

# cosmetic only (the part is axisymmetric): angular position of the revolve seams
BODY_SEAM_ANGLE = 135.0
HOLE_SEAM_ANGLE = -45.0

R0 = D / 2.0
HOLE_R = HOLE_D / 2.0
CSK_R = CSK_D / 2.0
TAN_HALF = math.tan(math.radians(CSK_ANGLE / 2.0))
CSK_DEPTH = (CSK_R - HOLE_R) / TAN_HALF

# ---- body: revolve of the half cross-section (XZ plane: local x = radius, local y = height)
# flat underside, quarter-round shoulder tangent to a flat crown
profile = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R0, 0)                                            # flat underside
    .radiusArc((R0 - R_SHOULDER, H), -R_SHOULDER)             # rounded shoulder (convex)
    .lineTo(0, H)                                             # flat crown
    .close()
)
body = (
    profile.revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), BODY_SEAM_ANGLE)
)

# ---- central through hole, countersunk from the underside (revolved cutter)
EXT = 1.0  # cutter overshoot past both faces
cutter = (
    cq.Workplane("XZ")
    .moveTo(0, -EXT)
    .lineTo(CSK_R + EXT * TAN_HALF, -EXT)                     # countersink mouth (below the base)
    .lineTo(HOLE_R, CSK_DEPTH)                                # conical countersink
    .lineTo(HOLE_R, H + EXT)                                  # straight bore through the crown
    .lineTo(0, H + EXT)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
    .rotate((0, 0, 0), (0, 0, 1), HOLE_SEAM_ANGLE)
)

result = body.cut(cutter)
